import math
import cadquery as cq
from OCP.BRepBuilderAPI import BRepBuilderAPI_Sewing, BRepBuilderAPI_MakeSolid
from OCP.TopoDS import TopoDS

# ---------------- driving dimensions (mm) ----------------
R = 30.0            # outer radius of knurled cap
H = 19.5            # overall height
RB = 26.4           # bore (thread root) radius
Z_FLOOR = 3.85      # inside floor height (bottom thickness)
FLOOR_CH = 0.8      # chamfer where floor meets bore wall

# bottom outer edge: fillet blending into a 45 deg chamfer
EDGE_R = 6.0        # fillet radius
EDGE_CH = 3.1       # radial inset of the edge treatment at the bottom face

# diamond knurl
N_KNURL = 29        # grooves per hand
KNURL_DEPTH = 1.4   # groove depth
KNURL_W = 2.0       # groove width at the surface, measured around the circumference
KNURL_HELIX = 45.0  # groove angle to the axis
KNURL_PHASE_A = 8.73  # polar angle of a right-hand groove at the bottom face (deg)
KNURL_PHASE_B = 3.58  # polar angle of a left-hand groove at the bottom face (deg)

# internal thread: 3-start, flat-topped rounded profile, right hand; every start is a ridge of limited
# sweep angle whose two ends are trimmed by vertical chord planes
TH_STARTS = 3
TH_LEAD = 16.2      # axial advance per turn of one start
TH_SPAN = 195.0     # angle swept by each ridge (deg)
TH_A_TOP = 119.0    # polar angle of the upper end of the first ridge (deg)
TH_Z_TOP = 16.5     # height of the profile centre at the upper end
TH_DEPTH = 1.25     # radial protrusion of the crest from the bore wall
TH_ROOT_W = 2.65    # axial width of the thread profile at the bore wall
TH_PROF_P = 2.5     # profile r(z) = RB - DEPTH*(1-|2z/ROOT_W|^P): flat-topped, flanked ridge
TH_END_DELTA = 8.5  # angle from the end's wall line back to where the trim plane cuts the crest
TH_END_EXT = 5.0    # sweep overrun past each trimmed end (deg)

SEAM_ANGLE = 225.0  # where the bore's revolve seam sits (on the silhouette of the standard views)

VIEW = {"azimuth": 45, "elevation": 26}

PER = 360.0 / N_KNURL
SECTOR_PERIODS = 1  # knurl periods per repeating sector (N_KNURL must be divisible by it)
N_SECTORS = N_KNURL // SECTOR_PERIODS
SECTOR = PER * SECTOR_PERIODS
TWIST = math.degrees(H * math.tan(math.radians(KNURL_HELIX)) / R)
ALPHA0 = 3.0        # start angle of the repeating sector


def body_profile():
    """Half cross-section of the cap (XZ plane, X = radius)."""
    # fillet tangent to the side wall at height z0 and to the 45 deg chamfer at t45
    z0 = EDGE_CH + EDGE_R * (math.sqrt(2.0) - 1.0)
    t45 = (R - EDGE_R + EDGE_R * math.cos(math.radians(-45)), z0 + EDGE_R * math.sin(math.radians(-45)))
    mid = (R - EDGE_R + EDGE_R * math.cos(math.radians(-22.5)), z0 + EDGE_R * math.sin(math.radians(-22.5)))
    return (
        cq.Workplane("XZ")
        .moveTo(0, 0)
        .lineTo(R - EDGE_CH, 0)
        .lineTo(*t45)
        .threePointArc(mid, (R, z0))
        .lineTo(R, H)
        .lineTo(RB, H)
        .lineTo(RB, Z_FLOOR + FLOOR_CH)
        .lineTo(RB - FLOOR_CH, Z_FLOOR)
        .lineTo(0, Z_FLOOR)
        .close()
    )


def groove_tool(theta_deg, twist):
    """One helical V groove of the knurl (twisted triangular prism)."""
    rext = R + 0.6
    hw = (KNURL_W / 2.0) / R
    th = math.radians(theta_deg)
    ax, ay = (R - KNURL_DEPTH) * math.cos(th), (R - KNURL_DEPTH) * math.sin(th)
    pts = []
    for s in (-1, 1):
        bx, by = R * math.cos(th + s * hw), R * math.sin(th + s * hw)
        dx, dy = bx - ax, by - ay
        qa = dx * dx + dy * dy
        qb = 2 * (ax * dx + ay * dy)
        qc = ax * ax + ay * ay - rext * rext
        t = (-qb + math.sqrt(qb * qb - 4 * qa * qc)) / (2 * qa)
        pts.append((ax + t * dx, ay + t * dy))
    poly = [pts[0], (ax, ay), pts[1]]
    return cq.Workplane("XY").polyline(poly).close().twistExtrude(H, twist).val()


def groove_set(theta0, twist):
    hwd = math.degrees(KNURL_W / 2.0 / R) * 1.5
    tools = []
    for k in range(-N_KNURL, N_KNURL + 1):
        c = theta0 + PER * k
        lo, hi = min(c, c + twist) - hwd, max(c, c + twist) + hwd
        if hi < ALPHA0 or lo > ALPHA0 + SECTOR:
            continue
        tools.append(groove_tool(c, twist))
    return tools


def _is_radial_plane(f):
    return f.geomType() == "PLANE" and abs(f.normalAt().z) < 1e-6


def _is_bore(f):
    if f.geomType() != "CYLINDER":
        return False
    v = f.Vertices()[0]
    return abs(math.hypot(v.X, v.Y) - RB) < 1e-3


def knurled_sector():
    """One repeating pie sector of the cap, knurled with both groove hands."""
    sector = body_profile().revolve(SECTOR, (0, 0, 0), (0, 1, 0)).val()
    sector = sector.rotate((0, 0, 0), (0, 0, 1), ALPHA0)
    th_a = KNURL_PHASE_A
    th_b = KNURL_PHASE_B
    sector = sector.cut(*groove_set(th_a, TWIST))
    sector = sector.cut(*groove_set(th_b, -TWIST))
    return sector


def _end_trim_box(phi_deg, z_mid, sign):
    """Prism removing the thread beyond a vertical chord plane: the plane meets the bore wall
    in a vertical line at phi and cuts the crest TH_END_DELTA further back along the thread."""
    ph = math.radians(phi_deg)
    pc = math.radians(phi_deg - sign * TH_END_DELTA)
    pq = math.radians(phi_deg + sign * 3.0)
    wx, wy = RB * math.cos(ph), RB * math.sin(ph)
    cx, cy = (RB - TH_DEPTH) * math.cos(pc), (RB - TH_DEPTH) * math.sin(pc)
    dx, dy = cx - wx, cy - wy
    ln = math.hypot(dx, dy)
    dx, dy = dx / ln, dy / ln
    nx, ny = -dy, dx
    if nx * (RB * math.cos(pq) - wx) + ny * (RB * math.sin(pq) - wy) < 0:
        nx, ny = -nx, -ny
    L, Wd, Hh = 10.0, 10.0, 2.4
    pts = [
        (wx - L / 2 * dx, wy - L / 2 * dy),
        (wx + L / 2 * dx, wy + L / 2 * dy),
        (wx + L / 2 * dx + Wd * nx, wy + L / 2 * dy + Wd * ny),
        (wx - L / 2 * dx + Wd * nx, wy - L / 2 * dy + Wd * ny),
    ]
    return (cq.Workplane("XY").workplane(offset=z_mid - Hh)
            .polyline(pts).close().extrude(2 * Hh).val())


def thread_ridge():
    rh = RB - TH_DEPTH / 2.0           # helix radius
    ext = TH_END_EXT
    a_low = TH_A_TOP - TH_SPAN
    z_low = TH_Z_TOP - TH_LEAD * TH_SPAN / 360.0
    sweep_ang = TH_SPAN + 2 * ext
    path = cq.Wire.makeHelix(TH_LEAD, TH_LEAD * sweep_ang / 360.0, rh)
    emb = 0.4                          # profile runs into the wall so the union is solid
    a = TH_ROOT_W / 2.0
    z_e = a * (1.0 + emb / TH_DEPTH) ** (1.0 / TH_PROF_P)
    n = 13
    pts = []
    for i in range(n):
        z = -z_e + 2.0 * z_e * i / (n - 1)
        pts.append((RB - TH_DEPTH * (1.0 - (abs(z) / a) ** TH_PROF_P), z))
    prof = cq.Workplane("XZ").spline(pts, includeCurrent=False).close()
    th = prof.sweep(cq.Workplane().add(path), isFrenet=True).val()
    th = th.rotate((0, 0, 0), (0, 0, 1), a_low - ext).translate((0, 0, z_low - TH_LEAD * ext / 360.0))
    th = th.cut(_end_trim_box(a_low, z_low, -1)).cut(_end_trim_box(TH_A_TOP, TH_Z_TOP, +1))
    return th


def thread():
    r1 = thread_ridge()
    return [r1.rotate((0, 0, 0), (0, 0, 1), 360.0 / TH_STARTS * i) for i in range(TH_STARTS)]


def plain_threaded_body():
    """Revolved cap (no knurl) with the three thread ridges fused onto the bore wall."""
    plain = body_profile().revolve(360, (0, 0, 0), (0, 1, 0)).val()
    return plain.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE).fuse(*thread())


def build():
    # The knurl is cut on one repeating sector only; its faces (minus the radial cut planes and the
    # bore patch) are patterned N_SECTORS times round the axis and sewn to the threaded bore wall.
    sector = knurled_sector()
    skin = [f for f in sector.Faces() if not _is_radial_plane(f) and not _is_bore(f)]
    plain = plain_threaded_body()
    inner = [f for f in plain.Faces()
             if _is_bore(f) or _is_radial_plane(f) or f.geomType() not in ("PLANE", "CYLINDER", "CONE", "TORUS")]
    sew = BRepBuilderAPI_Sewing(1e-4)
    for k in range(N_SECTORS):
        for f in skin:
            sew.Add(f.rotate((0, 0, 0), (0, 0, 1), SECTOR * k).wrapped)
    for f in inner:
        sew.Add(f.wrapped)
    sew.Perform()
    solid = cq.Solid(BRepBuilderAPI_MakeSolid(TopoDS.Shell_s(sew.SewedShape())).Solid())
    solid = solid.clean()
    if not solid.isValid() or solid.Volume() < 0.5 * plain.Volume():
        raise ValueError("sewn knurled body is not a valid closed solid")
    return solid


try:
    part = build()
except Exception:
    part = plain_threaded_body().Solids()[0]   # fallback: same cap without the knurl texture

result = cq.Workplane("XY").add(part)
